import math
import cadquery as cq

# ---------------------------------------------------------------- parameters
PITCH_X = 18.0          # column pitch (choc spacing)
PITCH_Y = 17.0          # row pitch
HOLE_W = 14.2           # switch cut-out, X
HOLE_H = 13.8           # switch cut-out, Y
HOLE_R = 0.8            # corner radius of switch cut-outs
HOLE_CH = 0.3           # chamfer on the top edge of switch cut-outs

H = 6.6                 # overall height (rim top)
T_FLOOR = 2.1           # floor thickness
TOP_FILLET = 0.7        # rounding of the outer top edge
BOT_CHAMFER = 1.0       # chamfer on the outer bottom edge
FLOOR_EDGE_CH = 0.4     # chamfer on the floor edge along the open right side

N_COLS = 5
COL_X = [PITCH_X * (i - 2) for i in range(N_COLS)]   # column centres
COL_Y0 = [-12.0, -4.3, 0.0, -3.0, -5.6]   # stagger (top-row key centre)
ROWS = 3

# thumb keys: (x, y, rotation deg)
THUMBS = [(11.9, -56.7, 0.0), (31.7, -59.5, -16.0), (50.4, -67.4, -30.0)]

# outline
X_LEFT = -48.0
X_RIGHT = 46.2
BACK_C = (-1.07, -149.70)  # back edge arc centre
BACK_R = 161.73
FRONT_Y = -68.0            # straight front edge under the thumb T1
FRONT_R = 69.8             # concave front arc of the thumb fan
TIP_RIGHT = 10.1           # thumb tip end, local x of T3
TIP_FRONT = 10.4           # thumb front edge, local -y of T3
TIP_TOP = 13.2             # thumb top edge, local y of T3

# slot lobe (front-left)
LOBE_C = (-42.9, -65.45)
LOBE_R = 7.8
LOBE_STEP_X0 = 1.2         # lobe bottom corner, slanted step up to the front edge
LOBE_STEP_X1 = 5.0         # front-edge corner of the slanted step
LOBE_STEP_R0 = 2.0
LOBE_STEP_R1 = 3.5
SLOT_R = 5.1
SLOT_WALL = 4.8            # wall between slot and pocket diagonal
SLOT_TOP_R = 0.6           # rounding of the slot top edge
SLOT_BOT_CH = 0.5          # chamfer of the slot bottom edge

# pocket
WALL_L = 2.0               # left wall
M_TOP = [3.3, 3.3, 3.25, 2.65, 2.7]   # pocket margin above each column
M_SIDE = 3.25              # pocket margin beside each column
M_FRONT = 2.2              # pocket margin in front of thumb keys
TIP_WALL = 1.2             # rim at the thumb tip
POCKET_FRONT_Y = -55.86    # pocket edge above the lobe
POCKET_R = 0.5             # vertical corner radius of the pocket
POCKET_BASE_R = 0.5        # fillet where walls meet the floor
DIAG_A = (-9.31, POCKET_FRONT_Y)   # pocket diagonal beside the lobe
DIAG_B = (2.55, -66.2)

# screws
SCREWS = [(-27.0, -13.0), (-27.0, -30.2), (23.2, -11.7), (-4.0, -48.8), (45.3, -53.5)]
SCREW_D = 1.8
BOSS_D = 3.1
BOSS_H = 0.35


# ---------------------------------------------------------------- helpers
def rot(p, a_deg):
    a = math.radians(a_deg)
    return (p[0] * math.cos(a) - p[1] * math.sin(a), p[0] * math.sin(a) + p[1] * math.cos(a))


def local(c, a_deg, lx, ly):
    r = rot((lx, ly), a_deg)
    return (c[0] + r[0], c[1] + r[1])


def line_isect(p1, d1, p2, d2):
    # p1 + t d1 = p2 + s d2
    det = d1[0] * (-d2[1]) - d1[1] * (-d2[0])
    rx, ry = p2[0] - p1[0], p2[1] - p1[1]
    t = (rx * (-d2[1]) - ry * (-d2[0])) / det
    return (p1[0] + t * d1[0], p1[1] + t * d1[1])


def back_y(x):
    return BACK_C[1] + math.sqrt(BACK_R ** 2 - (x - BACK_C[0]) ** 2)


def fillet_vertical(solid, specs):
    """fillet vertical edges located near (x, y) with radius r"""
    for (x, y, r) in specs:
        def sel(e, x=x, y=y):
            bb = e.BoundingBox()
            return (abs(bb.xmin - x) < 0.05 and abs(bb.xmax - x) < 0.05 and
                    abs(bb.ymin - y) < 0.05 and abs(bb.ymax - y) < 0.05 and
                    bb.zlen > 0.1)
        edges = [e for e in solid.Edges() if sel(e)]
        if edges:
            solid = solid.fillet(r, edges)
    return solid


# ---------------------------------------------------------------- outline
T3c = (THUMBS[2][0], THUMBS[2][1])
T3a = THUMBS[2][2]

p_back_l = (X_LEFT, back_y(X_LEFT))
p_back_r = (X_RIGHT, back_y(X_RIGHT))
p_back_m = (BACK_C[0], back_y(BACK_C[0]))

# thumb top edge meets right edge
u3 = rot((1, 0), T3a)
v3 = rot((0, 1), T3a)
top_pt = local(T3c, T3a, 0, TIP_TOP)
p_junction = line_isect(top_pt, u3, (X_RIGHT, 0), (0, 1))
p_tip_tr = local(T3c, T3a, TIP_RIGHT, TIP_TOP)
p_tip_br = local(T3c, T3a, TIP_RIGHT, -TIP_FRONT)

# front concave arc, tangent to y = FRONT_Y and to the T3 front line
front_line_pt = local(T3c, T3a, 0, -TIP_FRONT)
# centre lies FRONT_R below y=FRONT_Y and FRONT_R outside the T3 front line
# solve for x of centre: distance to T3 front line == FRONT_R
cy = FRONT_Y - FRONT_R
# signed dist = (c - front_line_pt) . v3 = -FRONT_R
cx = (-FRONT_R - (cy - front_line_pt[1]) * v3[1]) / v3[0] + front_line_pt[0]
p_fa = (cx, FRONT_Y)
p_fb = (cx + FRONT_R * v3[0], cy + FRONT_R * v3[1])
ang_mid = math.atan2(v3[1], v3[0]) / 2 + math.pi / 4
p_fm = (cx + FRONT_R * math.cos(ang_mid), cy + FRONT_R * math.sin(ang_mid))

lobe_bot_y = LOBE_C[1] - LOBE_R
lobe_left_y = LOBE_C[1] + math.sqrt(LOBE_R ** 2 - (X_LEFT - LOBE_C[0]) ** 2)
p_lobe_l = (X_LEFT, lobe_left_y)
p_lobe_far = (LOBE_C[0] - LOBE_R, LOBE_C[1])
p_lobe_bot = (LOBE_C[0], lobe_bot_y)

outline = (
    cq.Workplane("XY")
    .moveTo(*p_lobe_bot)
    .lineTo(LOBE_STEP_X0, lobe_bot_y)
    .lineTo(LOBE_STEP_X1, FRONT_Y)
    .lineTo(*p_fa)
    .threePointArc(p_fm, p_fb)
    .lineTo(*p_tip_br)
    .lineTo(*p_tip_tr)
    .lineTo(*p_junction)
    .lineTo(*p_back_r)
    .threePointArc(p_back_m, p_back_l)
    .lineTo(*p_lobe_l)
    .threePointArc(p_lobe_far, p_lobe_bot)
    .close()
)
body = outline.extrude(H).val()

body = fillet_vertical(body, [
    (LOBE_STEP_X0, lobe_bot_y, LOBE_STEP_R0),
    (LOBE_STEP_X1, FRONT_Y, LOBE_STEP_R1),
    (p_tip_br[0], p_tip_br[1], 2.5),
    (p_tip_tr[0], p_tip_tr[1], 1.8),
    (p_junction[0], p_junction[1], 1.5),
    (p_back_r[0], p_back_r[1], 1.5),
    (p_back_l[0], p_back_l[1], 3.5),
    (p_lobe_l[0], p_lobe_l[1], 2.0),
])

body = cq.Workplane("XY").add(body)
# outer top rounding and bottom chamfer
body = body.faces(">Z").edges().fillet(TOP_FILLET)
body = body.faces("<Z").edges().chamfer(BOT_CHAMFER)

# ---------------------------------------------------------------- pocket
col_tops = [y0 + HOLE_H / 2 + m for y0, m in zip(COL_Y0, M_TOP)]
hw = HOLE_W / 2 + M_SIDE
x_in = X_LEFT + WALL_L

pk = [(DIAG_A[0], POCKET_FRONT_Y), (x_in, POCKET_FRONT_Y), (x_in, col_tops[0])]
for i in range(1, N_COLS):
    # step located at the edge of the higher column's region
    if col_tops[i] > col_tops[i - 1]:
        xs = COL_X[i] - hw
    else:
        xs = COL_X[i - 1] + hw
    pk.append((xs, col_tops[i - 1]))
    pk.append((xs, col_tops[i]))
pk.append((110.0, col_tops[-1]))
pk.append((110.0, -30.0))
# tip inner line
tip_out = local(T3c, T3a, TIP_RIGHT - TIP_WALL, 30.0)
pk.append(tip_out)
# thumb front inner lines
fl = []
for (tx, ty, ta) in THUMBS:
    fl.append((local((tx, ty), ta, 0, -(HOLE_H / 2 + M_FRONT)), rot((1, 0), ta)))
tip_dir = rot((0, 1), T3a)
pk.append(line_isect(tip_out, tip_dir, fl[2][0], fl[2][1]))
pk.append(line_isect(fl[2][0], fl[2][1], fl[1][0], fl[1][1]))
pk.append(line_isect(fl[1][0], fl[1][1], fl[0][0], fl[0][1]))
diag_d = (DIAG_B[0] - DIAG_A[0], DIAG_B[1] - DIAG_A[1])
pk.append(line_isect(fl[0][0], fl[0][1], DIAG_A, diag_d))

pocket = (cq.Workplane("XY").workplane(offset=T_FLOOR)
          .polyline(pk).close().extrude(H)
          .edges("|Z").fillet(POCKET_R)
          .faces("<Z").edges().fillet(POCKET_BASE_R))
body = body.cut(pocket)


# small chamfer on the floor's top edge along the open (wall-less) sides
def open_side_edges(shape):
    es = [e for e in shape.Edges()
          if abs(e.BoundingBox().zmin - T_FLOOR) < 1e-3 and abs(e.BoundingBox().zmax - T_FLOOR) < 1e-3]

    def on_top_line(p):
        return abs((p.x - top_pt[0]) * v3[0] + (p.y - top_pt[1]) * v3[1]) < 1e-3

    core = []
    for e in es:
        bb = e.BoundingBox()
        ends = [e.startPoint(), e.endPoint()]
        if e.geomType() == "LINE" and abs(bb.xmin - X_RIGHT) < 1e-3 and abs(bb.xmax - X_RIGHT) < 1e-3:
            core.append(e)
        elif e.geomType() == "LINE" and all(on_top_line(p) for p in ends):
            core.append(e)
    chain = list(core)
    for e in es:
        if any(e.isSame(c) for c in chain):
            continue
        ends = [e.startPoint(), e.endPoint()]
        for c in core:
            if any((p - q).Length < 1e-4 for p in ends for q in (c.startPoint(), c.endPoint())):
                chain.append(e)
                break
    return chain


_b = body.val()
body = cq.Workplane("XY").add(_b.chamfer(FLOOR_EDGE_CH, None, open_side_edges(_b)))

# ---------------------------------------------------------------- slot
dl = math.hypot(*diag_d)
dn = (diag_d[0] / dl, diag_d[1] / dl)
nrm = (-dn[1], dn[0])   # points up-right (into pocket)
if nrm[0] < 0:
    nrm = (-nrm[0], -nrm[1])
s_pt = (DIAG_A[0] - nrm[0] * SLOT_WALL, DIAG_A[1] - nrm[1] * SLOT_WALL)
slot_top = LOBE_C[1] + SLOT_R
slot_bot = LOBE_C[1] - SLOT_R
p_st = line_isect(s_pt, dn, (0, slot_top), (1, 0))
p_sb = line_isect(s_pt, dn, (0, slot_bot), (1, 0))
slot = (cq.Workplane("XY").workplane(offset=-1)
        .moveTo(LOBE_C[0], slot_bot)
        .lineTo(*p_sb)
        .lineTo(*p_st)
        .lineTo(LOBE_C[0], slot_top)
        .threePointArc((LOBE_C[0] - SLOT_R, LOBE_C[1]), (LOBE_C[0], slot_bot))
        .close()
        .extrude(H + 2))
slot_s = fillet_vertical(slot.val(), [(p_st[0], p_st[1], 1.5), (p_sb[0], p_sb[1], 1.5)])
body = body.cut(cq.Workplane("XY").add(slot_s))


def slot_edges(shape, z):
    x0, x1 = LOBE_C[0] - SLOT_R - 0.3, max(p_st[0], p_sb[0]) + 0.5
    y0, y1 = slot_bot - 0.3, slot_top + 0.3
    out = []
    for e in shape.Edges():
        bb = e.BoundingBox()
        if (abs(bb.zmin - z) < 1e-3 and abs(bb.zmax - z) < 1e-3 and bb.xmin > x0 and
                bb.xmax < x1 and bb.ymin > y0 and bb.ymax < y1):
            out.append(e)
    return out


_b = body.val()
_b = _b.fillet(SLOT_TOP_R, slot_edges(_b, H))
_b = _b.chamfer(SLOT_BOT_CH, None, slot_edges(_b, 0.0))
body = cq.Workplane("XY").add(_b)

# ---------------------------------------------------------------- switch holes
keys = []
for cx_, y0 in zip(COL_X, COL_Y0):
    for r in range(ROWS):
        keys.append((cx_, y0 - r * PITCH_Y, 0.0))
keys += THUMBS


def key_cutter():
    sk = cq.Sketch().rect(HOLE_W, HOLE_H).vertices().fillet(HOLE_R)
    thru = cq.Workplane("XY").workplane(offset=-1).placeSketch(sk).extrude(H + 2).val()
    cham = (cq.Workplane("XY").workplane(offset=T_FLOOR - HOLE_CH)
            .placeSketch(sk).extrude(HOLE_CH + 0.3, taper=-45).val())
    return thru.fuse(cham).clean()


base_cut = key_cutter()
cutters = []
for (kx, ky, ka) in keys:
    c = base_cut.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), ka).translate(cq.Vector(kx, ky, 0))
    cutters.append(c)
for (sx, sy) in SCREWS:
    cutters.append(cq.Solid.makeCylinder(SCREW_D / 2, H + 2, cq.Vector(sx, sy, -1)))

# ---------------------------------------------------------------- screw bosses
bosses = [cq.Solid.makeCylinder(BOSS_D / 2, BOSS_H + 0.01, cq.Vector(sx, sy, T_FLOOR - 0.01))
          for (sx, sy) in SCREWS]
body = body.union(cq.Workplane("XY").add(bosses))
body = body.cut(cq.Workplane("XY").add(cutters))

result = body
VIEW = {"azimuth": 45, "elevation": 26}
